import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
N_SKIRT = 16          # sides of the faceted lower skirt (frustum)
R_BOT = 119.0         # skirt circumradius at the floor
R_TOP = 107.0         # skirt circumradius at the ring level
H_SKIRT = 51.5        # skirt height (ring level)

N_UP = 12             # sides of the upper housing
R_UP = 75.5           # upper housing circumradius
H_UP = 40.0           # upper housing height above the ring
T_TOP = 10.2          # top plate thickness
GROOVE_Z = 9.8        # parting groove below the top face
GROOVE_D = 0.5        # groove depth
GROOVE_H = 0.6        # groove height

N_BORE = 20           # big bore from below (20 facets)
R_BORE = 71.2         # bore circumradius
H_BORE = 51.5         # bore height (ledge at ring level)
R_IN = 60.0           # inner 12-gon bore (up to the top plate)

WEDGE_ANG = [15.0, 105.0, 195.0, 285.0]   # ramp blocks against housing faces
WEDGE_H = 23.0        # ramp height at the housing wall
WEDGE_ROUT = 100.6    # ramp toe radius on the ring

FOOT_ANG = [0.0, 90.0, 180.0, 270.0]      # feet under the floor
FOOT_L = 40.0         # tangential length
FOOT_W = 11.5         # radial width
FOOT_H = 9.5          # height
FOOT_RC = 106.7       # radius of the foot centre

PANELS = 8            # skirt panels (each bent once, two facets per panel)
SEAM_W = 1.4          # panel seam: V-notch width at the surface
SEAM_D = 0.9          # V-notch depth
CREASE_PANELS = [5, 7]  # panels carrying a diagonal crease line
CREASE_W = 0.6        # crease width
CREASE_D = 0.25       # crease depth

SCREW_DZ = 6.5        # countersunk screws: depth below the ring level
SCREW_GAP = 5.3       # screw distance from the seam
SCREW_R = 3.6         # countersink radius at the surface
SCREW_FLOOR_R = 2.0   # countersink radius at its floor
SCREW_DEPTH = 0.7     # countersink depth
SCREW_HEAD_R = 1.2    # domed head radius

HOLE_R = 8.85         # centre hole
SMALL_R = 4.0         # four small holes
SMALL_X = 14.7
SMALL_Y = 29.2
HOLES_DY = -1.9       # hole group offset
CBORE_R = 15.0        # relief under the centre hole (from the cavity side)
CBORE_LEFT = 3.9      # plate left above the relief

# two shallow triangular recesses either side of the centre hole: each floor
# rises from a sunken long edge (the right-hand step / the groove valley)
# to an apex beside the hole, flush with the top face
DISH_XL, DISH_XR = -22.4, 20.3   # sunken long edges
DISH_Y = 31.2                    # half length of the right-hand step
DISH_AL, DISH_AR = -12.1, 8.0    # apexes beside the centre hole
DISH_D = 2.2                     # depth of the long edges

# C-shaped through pocket (x, y) mirrored in y; its inner wall ends in a fin
# whose land slopes down into the left-hand recess
POCKET_A = (-35.8, 39.9)
POCKET_B = (-18.7, 35.2)
POCKET_C0 = (-28.5, 20.0)        # direction of the end wall B -> C
POCKET_L = (-49.5, 19.2)
FIN_X = -27.8                    # inner pocket wall
FIN_W = 1.6                      # flat land on top of the fin

Z_RING = H_SKIRT
Z_TOP = H_SKIRT + H_UP


def apothem(r, n):
    return r * math.cos(math.pi / n)


# ---------------------------------------------------------------------------
# Lower skirt: 16-sided frustum
# ---------------------------------------------------------------------------
def bent_edge(pts):
    """one edge running through a polyline (degree-1 B-spline): a bent panel edge"""
    n = len(pts)
    poles = TColgp_Array1OfPnt(1, n)
    knots = TColStd_Array1OfReal(1, n)
    mults = TColStd_Array1OfInteger(1, n)
    for i, p in enumerate(pts):
        poles.SetValue(i + 1, gp_Pnt(*p))
        knots.SetValue(i + 1, float(i))
        mults.SetValue(i + 1, 1)
    mults.SetValue(1, 2)
    mults.SetValue(n, 2)
    curve = Geom_BSplineCurve(poles, knots, mults, 1)
    return cq.Edge(BRepBuilderAPI_MakeEdge(curve).Edge())


def panel_wire(r, z):
    per = N_SKIRT // PANELS
    step = 360.0 / N_SKIRT
    edges = []
    for k in range(PANELS):
        pts = []
        for j in range(per + 1):
            a = math.radians((k * per + j) * step)
            pts.append((r * math.cos(a), r * math.sin(a), z))
        edges.append(bent_edge(pts))
    return cq.Wire.assembleEdges(edges)


def bent_ring(n, r, z, per, start=0):
    """closed n-sided polygon built from bent edges of `per` facets each"""
    edges = []
    for k in range(n // per):
        pts = []
        for j in range(per + 1):
            a = 2 * math.pi * (start + k * per + j) / n
            pts.append((r * math.cos(a), r * math.sin(a), z))
        edges.append(bent_edge(pts))
    return cq.Wire.assembleEdges(edges)


def bent_prism(n, r, z0, z1, per, start=0):
    return cq.Workplane("XY").add(
        cq.Solid.makeLoft([bent_ring(n, r, z0, per, start), bent_ring(n, r, z1, per, start)], True)
    )


# the skirt is a 16-sided frustum made of 8 bent panels (one face per panel)
skirt = cq.Workplane("XY").add(
    cq.Solid.makeLoft([panel_wire(R_BOT, 0.0), panel_wire(R_TOP, H_SKIRT)], True)
)

# upper 12-gon housing: walls bent in 60-degree segments
upper = bent_prism(N_UP, R_UP, Z_RING - 0.01, Z_TOP, 2, 1)
body = skirt.union(upper)

# ---------------------------------------------------------------------------
# Wedge blocks leaning against the housing
# ---------------------------------------------------------------------------
a_up = apothem(R_UP, N_UP)
face_w = 2 * R_UP * math.sin(math.pi / N_UP)
for ang in WEDGE_ANG:
    w = (
        cq.Workplane("XZ")
        .polyline([(a_up - 1.0, 0), (WEDGE_ROUT, 0), (a_up, WEDGE_H), (a_up - 1.0, WEDGE_H)])
        .close()
        .extrude(face_w / 2, both=True)
        .translate((0, 0, Z_RING - 0.01))
        .rotate((0, 0, 0), (0, 0, 1), ang)
    )
    body = body.union(w)

# ---------------------------------------------------------------------------
# Feet
# ---------------------------------------------------------------------------
for ang in FOOT_ANG:
    f = (
        cq.Workplane("XY")
        .box(FOOT_W, FOOT_L, FOOT_H + 0.1, centered=(True, True, False))
        .translate((FOOT_RC, 0, -FOOT_H))
        .rotate((0, 0, 0), (0, 0, 1), ang)
    )
    body = body.union(f)

# ---------------------------------------------------------------------------
# Cavity from below: 20-gon bore + 12-gon inner bore
# ---------------------------------------------------------------------------
# 20-sided bore formed as four faceted quarter surfaces
bore = bent_prism(N_BORE, R_BORE, -1.0, H_BORE, N_BORE // 4)
inner = (
    cq.Workplane("XY")
    .workplane(offset=H_BORE - 0.5)
    .polygon(N_UP, 2 * R_IN)
    .extrude(Z_TOP - T_TOP - H_BORE + 0.5)
)
body = body.cut(bore).cut(inner)

# ---------------------------------------------------------------------------
# Parting groove round the housing
# ---------------------------------------------------------------------------
gz0 = Z_TOP - GROOVE_Z - GROOVE_H / 2
groove = (
    cq.Workplane("XY")
    .workplane(offset=gz0)
    .circle(R_UP + 3)
    .extrude(GROOVE_H)
    .cut(bent_prism(N_UP, R_UP - GROOVE_D / math.cos(math.pi / N_UP), gz0 - 1, gz0 + GROOVE_H + 1, 2, 1))
)
body = body.cut(groove)

# ---------------------------------------------------------------------------
# Panel seams on the skirt (every 45 deg)
# ---------------------------------------------------------------------------
tilt = math.degrees(math.atan2(R_BOT - R_TOP, H_SKIRT))
edge_len = math.hypot(R_BOT - R_TOP, H_SKIRT)
seams = None
hw_out = SEAM_W / 2 * (1.0 + 1.0 / SEAM_D)
for k in range(PANELS):
    s = (
        cq.Workplane("XY")
        .polyline([(1.0, hw_out), (-SEAM_D, 0.0), (1.0, -hw_out)])
        .close()
        .extrude(edge_len + 6)
        .translate((0, 0, -(edge_len + 6) / 2))
        .rotate((0, 0, 0), (0, 1, 0), -tilt)
        .translate(((R_BOT + R_TOP) / 2, 0, H_SKIRT / 2))
        .rotate((0, 0, 0), (0, 0, 1), 360.0 / PANELS * k)
    )
    seams = s if seams is None else seams.union(s)
body = body.cut(seams)

# fine diagonal crease on some panels: from the top corner at the panel's
# leading seam down to the bottom of the panel bend
step = 2 * math.pi / N_SKIRT
for k in CREASE_PANELS:
    a2 = (k + 1) * 2 * step
    am = (2 * k + 1) * step
    t2 = cq.Vector(R_TOP * math.cos(a2), R_TOP * math.sin(a2), H_SKIRT)
    bm = cq.Vector(R_BOT * math.cos(am), R_BOT * math.sin(am), 0.0)
    b2 = cq.Vector(R_BOT * math.cos(a2), R_BOT * math.sin(a2), 0.0)
    d = (bm - t2).normalized()
    nrm = (b2 - t2).cross(bm - t2).normalized()
    if nrm.dot(cq.Vector(math.cos(am + step / 2), math.sin(am + step / 2), 0)) < 0:
        nrm = -nrm
    bx_ = nrm.cross(d)
    ln = (bm - t2).Length
    hw = CREASE_W / 2 * (1.0 + 0.3 / CREASE_D)
    crease = (
        cq.Workplane(cq.Plane(origin=t2 - d * 1.0, xDir=bx_, normal=d))
        .polyline([(-hw, 0.3), (0.0, -CREASE_D), (hw, 0.3)])
        .close()
        .extrude(ln + 1.5)
    )
    body = body.cut(crease)

# ---------------------------------------------------------------------------
# Countersunk screws either side of each seam
# ---------------------------------------------------------------------------
a_bot = apothem(R_BOT, N_SKIRT)
a_top = apothem(R_TOP, N_SKIRT)
beta = math.atan2(a_bot - a_top, H_SKIRT)       # face lean
gamma = 90.0 - math.degrees(beta)
zs = H_SKIRT - SCREW_DZ
a_s = a_top + (a_bot - a_top) * (SCREW_DZ / H_SKIRT)
half = a_s * math.tan(math.pi / N_SKIRT)
s_off = half - SCREW_GAP


def place(wp, alpha, s):
    return (
        wp.rotate((0, 0, 0), (0, 1, 0), gamma)
        .translate((a_s, s, zs))
        .rotate((0, 0, 0), (0, 0, 1), alpha)
    )


csk_slope = (SCREW_R - SCREW_FLOOR_R) / SCREW_DEPTH
recess_proto = cq.Workplane("XY").add(
    cq.Solid.makeCone(SCREW_FLOOR_R, SCREW_R + csk_slope * 1.0, SCREW_DEPTH + 1.0,
                      pnt=cq.Vector(0, 0, -SCREW_DEPTH))
)
head_proto = cq.Workplane("XY").add(
    cq.Solid.makeSphere(SCREW_HEAD_R, angleDegrees1=-90, angleDegrees2=90)
).translate((0, 0, -SCREW_DEPTH - 0.2))

recesses = None
heads = None
for k in range(PANELS):
    th = 360.0 / PANELS * k
    for sign in (1, -1):
        alpha = th + sign * 180.0 / N_SKIRT
        s = -sign * s_off
        r = place(recess_proto, alpha, s)
        h = place(head_proto, alpha, s)
        recesses = r if recesses is None else recesses.union(r)
        heads = h if heads is None else heads.union(h)
body = body.cut(recesses).union(heads)

# ---------------------------------------------------------------------------
# Top plate features
# ---------------------------------------------------------------------------
z_under = Z_TOP - T_TOP

# centre hole + 4 small holes
holes = (
    cq.Workplane("XY")
    .workplane(offset=z_under - 1)
    .center(0, HOLES_DY)
    .circle(HOLE_R)
    .extrude(T_TOP + 2)
)
small = (
    cq.Workplane("XY")
    .workplane(offset=z_under - 1)
    .pushPoints([(sx * SMALL_X, sy * SMALL_Y + HOLES_DY) for sx in (-1, 1) for sy in (-1, 1)])
    .circle(SMALL_R)
    .extrude(T_TOP + 2)
)
body = body.cut(holes).cut(small)

# relief recess under the centre hole (plate thinned to CBORE_LEFT)
cbore = (
    cq.Workplane("XY")
    .workplane(offset=z_under - 1.0)
    .center(0, HOLES_DY)
    .circle(CBORE_R)
    .extrude(T_TOP - CBORE_LEFT + 1.0)
)
body = body.cut(cbore)

# shallow triangular recesses (tetrahedral cuts)
def convex_solid(face_pts):
    faces = [
        cq.Face.makeFromWires(cq.Wire.makePolygon([cq.Vector(*p) for p in pts], close=True))
        for pts in face_pts
    ]
    sol = cq.Solid.makeSolid(cq.Shell.makeShell(faces))
    if sol.Volume() < 0:
        sol = cq.Solid(sol.wrapped.Reversed())
    return sol


def tri_recess(apex, e1, e2, depth, ext=1.0):
    """triangular recess: vertical step of `depth` along e1-e2, floor rising
    to the top face at `apex`"""
    top_a = (apex[0], apex[1], Z_TOP + ext)
    top_a0 = (apex[0], apex[1], Z_TOP)
    t1, t2 = (e1[0], e1[1], Z_TOP + ext), (e2[0], e2[1], Z_TOP + ext)
    b1, b2 = (e1[0], e1[1], Z_TOP - depth), (e2[0], e2[1], Z_TOP - depth)
    return convex_solid([
        [t1, t2, top_a],
        [t1, b1, b2, t2],
        [t1, top_a, top_a0, b1],
        [t2, b2, top_a0, top_a],
        [b1, top_a0, b2],
    ])


yc = HOLES_DY
ext = 1.0
rec_r = tri_recess((DISH_AR, yc), (DISH_XR, yc + DISH_Y), (DISH_XR, yc - DISH_Y), DISH_D)
body = body.cut(cq.Workplane("XY").add(rec_r))

# C-shaped through pocket
(ax, ay), (bx, by), (cx0, cy0) = POCKET_A, POCKET_B, POCKET_C0
lx, ly = POCKET_L


def on_bc(xq):
    t = (xq - bx) / (cx0 - bx)
    return by + t * (cy0 - by)


cy = on_bc(FIN_X)
pocket_outline = [
    (ax, ay), (bx, by), (FIN_X, cy), (FIN_X, -cy), (bx, -by), (ax, -ay),
    (lx, -ly), (lx, ly),
]
pocket = (
    cq.Workplane("XY")
    .workplane(offset=z_under - 1.0)
    .polyline(pocket_outline)
    .close()
    .extrude(T_TOP + 2.0)
)
body = body.cut(pocket)

# sloped land from the fin down to the sunken edge of the left recess,
# bounded by the pocket end walls
x_s = FIN_X + FIN_W
kx = (DISH_XL - x_s) / DISH_D
slope_cut = (
    cq.Workplane("XZ")
    .polyline([
        (x_s - kx * ext, Z_TOP + ext),
        (DISH_XL, Z_TOP - DISH_D),
        (DISH_XL, Z_TOP + ext),
    ])
    .close()
    .extrude(60, both=True)
)
gx = -40.0
clip = (
    cq.Workplane("XY")
    .workplane(offset=Z_TOP - 5.0)
    .polyline([(bx, by), (gx, on_bc(gx)), (gx, -on_bc(gx)), (bx, -by)])
    .close()
    .extrude(10.0)
)
ye = on_bc(DISH_XL)
rec_l = tri_recess((DISH_AL, yc), (DISH_XL, ye), (DISH_XL, -ye), DISH_D)
left_cut = slope_cut.intersect(clip).union(cq.Workplane("XY").add(rec_l))
body = body.cut(left_cut)

result = body
